import math
import cadquery as cq

# ======================= driving dimensions (mm) =======================
L = 99.0          # overall length (X)
W = 40.0          # overall width (Y)
H = 56.8          # overall height (Z)
t = 6.2           # prong (fork plate) thickness
h_low = 30.0      # height of the low socket block
x_up = 43.8       # -X face of the upright
x_web = 55.0      # +X end of the side walls (bottom of the fork opening)
R_con = 20.0      # big concave blend low block -> upright
r_top = 5.5       # convex round on top of the upright
r_in = 4.0        # fillets inside the fork
r_end_top = 8.0   # round, top edge of the -X end
r_end_bot = 4.2   # round, bottom edge of the -X end

# hollow interior (open toward the fork)
wall_side = 4.3   # side wall thickness (+Y side, and -Y side at the fork)
wall_end = 8.0    # -X end wall thickness
floor_z = 4.4     # cavity floor
ceil_z = 25.2     # cavity ceiling under the low block top
x_step = 42.0     # floor steps up to the prong surface here
x_v = 50.9        # inner vertical face of the upright
R_ceil = 19.8     # convex inner blend of the ceiling
y_block = -4.6    # thick -Y wall region ends at this Y ...
R_block = 12.5    # ... with this rounded end (plan view)

# socket window on the -Y face
win_x0, win_x1 = 4.4, 47.5
win_z0, win_z1 = floor_z, 21.7
win_depth = 10.5
pass_x0, pass_x1 = 8.0, 41.7   # narrower passage behind it into the cavity

# holes
hole_d = 16.0     # top prong cross hole
slot_w = 8.8      # blind slot in the bottom prong
slot_x0 = 61.0    # slot end centres
slot_depth = 4.0
pin_hole_d = 6.2  # small through hole in the bottom prong

# latch button on the +Y face
boss_x = 19.0
boss_z = 12.9
flange_d = 12.8
flange_h = 1.3
boss_d = 9.9
boss_h = 3.9

r_edge = 2.2      # general round on all outer edges
r_bar = 3.8       # big round on the outer edges of the fork opening (the side-wall ends)
fade_len = 8.0    # length over which that round fades into the prong edge round

VIEW = {"azimuth": 45, "elevation": 26}

xc = L - W / 2.0  # centre of the prong end arcs / hole axis


def rounded_profile(wp, pts):
    """closed polyline (x, y, r) with corner radius r at each vertex."""
    n = len(pts)
    segs = []
    for i in range(n):
        p0 = pts[i - 1]
        p1 = pts[i]
        p2 = pts[(i + 1) % n]
        r = p1[2]
        if r <= 0:
            segs.append(((p1[0], p1[1]), None, (p1[0], p1[1])))
            continue
        v1 = (p0[0] - p1[0], p0[1] - p1[1])
        v2 = (p2[0] - p1[0], p2[1] - p1[1])
        l1 = math.hypot(*v1)
        l2 = math.hypot(*v2)
        u1 = (v1[0] / l1, v1[1] / l1)
        u2 = (v2[0] / l2, v2[1] / l2)
        cosang = u1[0] * u2[0] + u1[1] * u2[1]
        ang = math.acos(max(-1.0, min(1.0, cosang)))
        d = r / math.tan(ang / 2.0)
        a = (p1[0] + u1[0] * d, p1[1] + u1[1] * d)
        b = (p1[0] + u2[0] * d, p1[1] + u2[1] * d)
        bis = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*bis)
        bis = (bis[0] / lb, bis[1] / lb)
        dc = r / math.sin(ang / 2.0)
        c = (p1[0] + bis[0] * dc, p1[1] + bis[1] * dc)
        m = (c[0] - bis[0] * r, c[1] - bis[1] * r)
        segs.append((a, m, b))
    w = wp.moveTo(*segs[0][2])
    for i in range(1, n + 1):
        a, m, b = segs[i % n]
        w = w.lineTo(*a)
        if m is not None:
            w = w.threePointArc(m, b)
    return w.close()


def sharp_edges(solid, min_deg=10.0, box=None):
    """edges whose two adjacent faces meet at an angle (not tangent)."""
    out = []
    for e in solid.Edges():
        p = e.positionAt(0.5)
        if box is not None:
            (x0, y0, z0), (x1, y1, z1) = box
            if not (x0 <= p.x <= x1 and y0 <= p.y <= y1 and z0 <= p.z <= z1):
                continue
        fs = list(e.ancestors(solid, "Face"))
        if len(fs) != 2:
            continue
        n1 = fs[0].normalAt(p)
        n2 = fs[1].normalAt(p)
        c = max(-1.0, min(1.0, n1.dot(n2)))
        if math.degrees(math.acos(c)) > min_deg:
            out.append(e)
    return out


c45 = math.cos(math.pi / 4)


def corner_cut(wp, y0, ys, zc, dz, r, e=0.3):
    """2D region (Y, Z) removed to round the corner at (y0, zc); material lies toward -ys in Y and +dz in Z."""
    return (
        wp.moveTo(y0 + ys * e, zc - dz * e)
        .lineTo(y0 - ys * r, zc - dz * e)
        .lineTo(y0 - ys * r, zc)
        .threePointArc((y0 - ys * (r - r * c45), zc + dz * (r - r * c45)), (y0, zc + dz * r))
        .lineTo(y0 + ys * e, zc + dz * r)
        .close()
    )


# ======================= outer body =======================
side_pts = [
    (0.0, 0.0, r_end_bot),
    (L + 1.0, 0.0, 0.0),
    (L + 1.0, t, 0.0),
    (x_web, t, r_in),
    (x_web, H - t, r_in),
    (L + 1.0, H - t, 0.0),
    (L + 1.0, H, 0.0),
    (x_up, H, r_top),
    (x_up, h_low, R_con),
    (0.0, h_low, r_end_top),
]
side = rounded_profile(cq.Workplane("XZ"), side_pts).extrude(W / 2.0, both=True)

plan = (
    cq.Workplane("XY")
    .moveTo(0, -W / 2.0)
    .lineTo(xc, -W / 2.0)
    .threePointArc((L, 0), (xc, W / 2.0))
    .lineTo(0, W / 2.0)
    .close()
    .extrude(H)
)
body = side.intersect(plan)

# round every sharp outer edge (cast look)
try:
    body = cq.Workplane("XY").add(body.val().fillet(r_edge, sharp_edges(body.val())))
except Exception:
    pass

# bigger round where the side faces meet the fork opening (rounded "bars"),
# swept along the opening outline and faded out along the prong edges

x_tan = x_web + r_in  # where the inner fork fillets meet the prong faces
for ys in (-1.0, 1.0):
    y0 = ys * W / 2.0
    bar_path = (
        cq.Workplane("XZ", origin=(0, y0, 0))
        .moveTo(x_tan, t)
        .threePointArc((x_tan - r_in * c45, t + r_in - r_in * c45), (x_web, t + r_in))
        .lineTo(x_web, H - t - r_in)
        .threePointArc((x_tan - r_in * c45, H - t - r_in + r_in * c45), (x_tan, H - t))
    )
    try:
        bar_tool = corner_cut(cq.Workplane("YZ", origin=(x_tan, 0, 0)), y0, ys, t, -1.0, r_bar).sweep(bar_path)
        for zc, dz in ((t, -1.0), (H - t, 1.0)):
            fade = corner_cut(cq.Workplane("YZ", origin=(x_tan, 0, 0)), y0, ys, zc, dz, r_bar)
            fade = corner_cut(fade.workplane(offset=fade_len), y0, ys, zc, dz, r_edge * 0.9)
            bar_tool = bar_tool.union(fade.loft(ruled=True))
        trial = body.cut(bar_tool)
        if trial.val().isValid():
            body = trial
    except Exception:
        pass

# ======================= hollow interior =======================
yc_max = W / 2.0 - wall_side
yc_min = -W / 2.0 + wall_side
arc_cx = x_v - R_ceil
arc_cz = ceil_z + R_ceil
a45 = math.radians(45)
cav_prof = (
    cq.Workplane("XZ")
    .moveTo(wall_end, floor_z)
    .lineTo(x_step, floor_z)
    .lineTo(x_step, t)
    .lineTo(x_web + 8, t)
    .lineTo(x_web + 8, H - t)
    .lineTo(x_v, H - t)
    .lineTo(x_v, arc_cz)
    .threePointArc((arc_cx + R_ceil * math.sin(a45), arc_cz - R_ceil * math.cos(a45)), (arc_cx, ceil_z))
    .lineTo(wall_end, ceil_z)
    .close()
    .extrude(W / 2.0, both=True)
)
bx = x_v - R_block  # centre of the rounded end of the thick -Y wall
cav_plan = (
    cq.Workplane("XY")
    .rect(200, yc_max - y_block, centered=False)
    .extrude(H)
    .translate((-50, y_block, 0))
)
band = (
    cq.Workplane("XY")
    .rect(200, y_block - yc_min, centered=False)
    .extrude(H)
    .translate((bx, yc_min, 0))
    .cut(cq.Workplane("XY").center(bx, yc_min).circle(R_block).extrude(H))
)
cav_plan = cav_plan.union(band)
cavity = cav_prof.intersect(cav_plan)
body = body.cut(cavity)

# ======================= socket window on -Y face =======================
win = (
    cq.Workplane("XY")
    .box(win_x1 - win_x0, win_depth + 1.0, win_z1 - win_z0, centered=False)
    .translate((win_x0, -W / 2.0 - 1.0, win_z0))
)
passage = (
    cq.Workplane("XY")
    .box(pass_x1 - pass_x0, (y_block + 1.0) - (-W / 2.0 + win_depth - 0.5), win_z1 - win_z0, centered=False)
    .translate((pass_x0, -W / 2.0 + win_depth - 0.5, win_z0))
)
body = body.cut(win).cut(passage)

# ======================= holes and slot =======================
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, H - t - 1.0)).center(xc, 0).circle(hole_d / 2.0).extrude(t + 2.0)
)
slot_len = xc - slot_x0
slot = (
    cq.Workplane("XY", origin=(0, 0, t - slot_depth))
    .center((xc + slot_x0) / 2.0, 0)
    .slot2D(slot_len + slot_w, slot_w)
    .extrude(slot_depth + 1.0)
)
body = body.cut(slot)
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, -1.0)).center(xc, 0).circle(pin_hole_d / 2.0).extrude(t + 2.0)
)

# ======================= latch button on +Y face =======================
flange = (
    cq.Workplane("XZ", origin=(0, W / 2.0, 0))
    .center(boss_x, boss_z)
    .circle(flange_d / 2.0)
    .extrude(-flange_h)
)
pin = (
    cq.Workplane("XZ", origin=(0, W / 2.0 + flange_h, 0))
    .center(boss_x, boss_z)
    .circle(boss_d / 2.0)
    .extrude(-boss_h)
)
try:
    pin = pin.faces(">Y").edges().fillet(0.8)
except Exception:
    pass
body = body.union(flange).union(pin)

result = body
